import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Front bezel / label plate for a panel meter
# ---------------------------------------------------------------------------

# --- plate -----------------------------------------------------------------
W = 120.0            # plate width  (X)
H = 97.4             # plate height (Y)
T = 2.1              # plate thickness
PLATE_R = 1.0        # plan corner radius
TOP_FILLET = 0.6     # round-over on the top outer edge
BOT_FILLET = 0.25    # small break on the bottom outer edge
CUT_TOP_R = 0.5      # round-over on top edges of window / holes
CUT_BOT_R = 0.3      # round-over on bottom edges of window / holes

# --- locating rim on the underside -----------------------------------------
RIM_INSET = 2.0      # rim outer face inset from plate edge
RIM_W = 3.5          # rim width where it meets the plate
RIM_H = 2.3          # rim height below plate
RIM_LEAD_H = 0.8     # height of the tapered lead-in at the bottom of the rim
RIM_LEAD_IN = 0.8    # how far the lead-in pulls the outer face inward
RIM_IN_FILLET = 0.3  # round on the inner bottom edge of the rim

# --- display window ---------------------------------------------------------
WIN_W = 79.05
WIN_H = 27.05
WIN_X = 7.98
WIN_Y = 17.02
WIN_R = 0.5          # plan corner radius of the window

# --- push-button holes -------------------------------------------------------
BIG_D = 13.0
BIG_PITCH = 17.6
BIG_X0 = 11.15
BIG_Y = -22.2

SMALL_D = 5.6
SMALL_PITCH = 9.8
SMALL_X0 = 11.0
SMALL_Y = -7.3

# --- logo (ammeter icon) ------------------------------------------------------
LOGO_X = -34.9
LOGO_Y = -25.6
LOGO_S = 31.0        # square outline of the icon
POCKET_D = 1.6       # engraving depth
RELIEF_DROP = 0.3    # raised features sit this much below the top face

ISLAND_W = 23.8      # meter body inside the U shaped groove
ISLAND_BOT = -5.0
ISLAND_R = 1.0       # rounded lower corners of the meter body
LOGO_CORNER_R = 0.6  # rounded lower outer corners of the groove
DISP_W = 19.8        # display recess
DISP_ARC_R = 18.4
DISP_ARC_TOP = 3.37  # apex of display bottom arc
LENS_R = 13.1
LENS_TOP = 1.34
LENS_BOT = -3.06
NOTCH_W = 2.5
NOTCH_TOP = -0.68

RING_X = 8.9
RING_Y = -10.2
RING_R = 3.1
RING_HOLE_R = 1.0
OVAL_X = 2.43
OVAL_DY = 2.0
OVAL_A = 1.55
OVAL_B = 0.95

A_ROUND = 0.6        # corner rounding of the letter A
A_ROUND_IN = 0.3

DOT_X = 6.8
DOT_Y = 5.8
DOT_A = 1.6
DOT_B = 1.25

Z_TOP = T


def logo_wp(z=0.0):
    return cq.Workplane("XY").workplane(offset=z).center(LOGO_X, LOGO_Y)


def rounded_prism(pts, r_convex, r_concave, height, z0):
    """Closed polygon (logo-local coords) with rounded corners, extruded up."""
    w = cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts], close=True)
    if r_convex > 0:
        w = w.offset2D(-r_convex, "arc")[0].offset2D(r_convex, "arc")[0]
    if r_concave > 0:
        w = w.offset2D(r_concave, "arc")[0].offset2D(-r_concave, "arc")[0]
    solid = cq.Solid.extrudeLinear(cq.Face.makeFromWires(w), cq.Vector(0, 0, height))
    return cq.Workplane("XY").add(solid.translate(cq.Vector(LOGO_X, LOGO_Y, z0)))


# ---------------------------------------------------------------------------
# base plate
plate = (
    cq.Workplane("XY")
    .rect(W, H)
    .extrude(T)
    .edges("|Z")
    .fillet(PLATE_R)
)
plate = plate.faces(">Z").edges().fillet(TOP_FILLET)
plate = plate.faces("<Z").edges().fillet(BOT_FILLET)

# through cut-outs
cut_depth = T + 2
window = (
    cq.Workplane("XY").workplane(offset=-1)
    .center(WIN_X, WIN_Y)
    .rect(WIN_W, WIN_H)
    .extrude(cut_depth)
    .edges("|Z")
    .fillet(WIN_R)
)
plate = plate.cut(window)

big_pts = [(BIG_X0 + i * BIG_PITCH, BIG_Y) for i in (-1, 0, 1)]
small_pts = [(SMALL_X0 + i * SMALL_PITCH, SMALL_Y) for i in (-1, 0, 1)]
holes = (
    cq.Workplane("XY").workplane(offset=-1)
    .pushPoints(big_pts).circle(BIG_D / 2).extrude(cut_depth)
    .union(
        cq.Workplane("XY").workplane(offset=-1)
        .pushPoints(small_pts).circle(SMALL_D / 2).extrude(cut_depth)
    )
)
plate = plate.cut(holes)

# soften the edges of the cut-outs (top and bottom)
inner_lo = (-W / 2 + 5, -H / 2 + 5)
inner_hi = (W / 2 - 5, H / 2 - 5)
plate = plate.edges(
    cq.selectors.BoxSelector(
        (inner_lo[0], inner_lo[1], T - 0.01), (inner_hi[0], inner_hi[1], T + 0.01)
    )
).fillet(CUT_TOP_R)
plate = plate.edges(
    cq.selectors.BoxSelector(
        (inner_lo[0], inner_lo[1], -0.01), (inner_hi[0], inner_hi[1], 0.01)
    )
).fillet(CUT_BOT_R)

# underside locating rim: straight outer wall, then a shallow tapered lead-in
rim_w_out = W - 2 * RIM_INSET
rim_h_out = H - 2 * RIM_INSET
rim_straight = RIM_H - RIM_LEAD_H
rim_upper = (
    cq.Workplane("XY")
    .rect(rim_w_out, rim_h_out)
    .extrude(-rim_straight)
)
lead_taper = math.degrees(math.atan2(RIM_LEAD_IN, RIM_LEAD_H))
rim_lower = (
    cq.Workplane("XY")
    .workplane(offset=-rim_straight)
    .rect(rim_w_out, rim_h_out)
    .extrude(-RIM_LEAD_H, taper=lead_taper)
)
rim_in = (
    cq.Workplane("XY").workplane(offset=0.5)
    .rect(W - 2 * (RIM_INSET + RIM_W), H - 2 * (RIM_INSET + RIM_W))
    .extrude(-RIM_H - 1)
)
rim = rim_upper.union(rim_lower).cut(rim_in)
inner_box = cq.selectors.BoxSelector(
    (-W / 2 + RIM_INSET + RIM_W - 0.5, -H / 2 + RIM_INSET + RIM_W - 0.5, -RIM_H - 0.01),
    (W / 2 - RIM_INSET - RIM_W + 0.5, H / 2 - RIM_INSET - RIM_W + 0.5, -RIM_H + 0.01),
)
rim = rim.edges(inner_box).fillet(RIM_IN_FILLET)
plate = plate.union(rim)

# ---------------------------------------------------------------------------
# logo: engraved pockets
z_floor = Z_TOP - POCKET_D
half = LOGO_S / 2

# U-shaped groove around the meter body
u_outer = (
    logo_wp(z_floor).rect(LOGO_S, LOGO_S).extrude(POCKET_D + 1)
    .edges("|Z").edges("<Y").fillet(LOGO_CORNER_R)
)
island_h = half + 2 - ISLAND_BOT
island = (
    logo_wp(z_floor - 0.5)
    .center(0, ISLAND_BOT + island_h / 2)
    .rect(ISLAND_W, island_h)
    .extrude(POCKET_D + 2)
    .edges("|Z").fillet(ISLAND_R)
)
u_pocket = u_outer.cut(island)

# display recess: rectangle with an arched bottom
disp_rect = (
    logo_wp(z_floor)
    .center(0, half / 2)
    .rect(DISP_W, half)
    .extrude(POCKET_D + 1)
)
disp_arc = (
    logo_wp(z_floor - 0.5)
    .center(0, DISP_ARC_TOP - DISP_ARC_R)
    .circle(DISP_ARC_R)
    .extrude(POCKET_D + 2)
)
disp_pocket = disp_rect.cut(disp_arc)

# lens shaped scale recess with pivot notch
lens_disk = (
    logo_wp(z_floor)
    .center(0, LENS_TOP - LENS_R)
    .circle(LENS_R)
    .extrude(POCKET_D + 1)
)
lens_keep = (
    logo_wp(z_floor - 0.5)
    .center(0, (LENS_BOT + LENS_TOP + 1) / 2)
    .rect(2 * LENS_R, LENS_TOP + 1 - LENS_BOT)
    .extrude(POCKET_D + 2)
)
lens = lens_disk.intersect(lens_keep)
notch_r = NOTCH_W / 2
notch = (
    logo_wp(z_floor - 0.5)
    .center(0, (LENS_BOT - 0.2 + NOTCH_TOP - notch_r) / 2)
    .rect(NOTCH_W, NOTCH_TOP - notch_r - LENS_BOT + 0.2)
    .extrude(POCKET_D + 2)
    .union(
        logo_wp(z_floor - 0.5)
        .center(0, NOTCH_TOP - notch_r)
        .circle(notch_r)
        .extrude(POCKET_D + 2)
    )
)
lens = lens.cut(notch)

plate = plate.cut(u_pocket).cut(disp_pocket).cut(lens)

# ---------------------------------------------------------------------------
# logo: raised relief inside the pockets
relief_h = POCKET_D - RELIEF_DROP

# control knobs (rings) and buttons (ovals)
rings = (
    logo_wp(z_floor)
    .pushPoints([(-RING_X, RING_Y), (RING_X, RING_Y)])
    .circle(RING_R)
    .circle(RING_HOLE_R)
    .extrude(relief_h)
)
ovals = None
for sx in (-1, 1):
    for sy in (-1, 1):
        o = (
            logo_wp(z_floor)
            .center(sx * OVAL_X, RING_Y + sy * OVAL_DY)
            .ellipse(OVAL_A, OVAL_B)
            .extrude(relief_h)
        )
        ovals = o if ovals is None else ovals.union(o)

# scale dots
dots = None
for sx in (-1, 1):
    d = (
        logo_wp(z_floor)
        .center(sx * DOT_X, DOT_Y)
        .ellipse(DOT_A, DOT_B, rotation_angle=75)
        .extrude(relief_h)
    )
    dots = d if dots is None else dots.union(d)

# letter "A"
A_pts = [
    (-3.45, 5.65),
    (-1.35, 5.65),
    (-0.55, 6.85),
    (0.0, 7.15),
    (0.55, 6.85),
    (1.35, 5.65),
    (3.45, 5.65),
    (1.0, 13.5),
    (-1.0, 13.5),
]
A_counter = [(-0.7, 8.6), (0.7, 8.6), (0.0, 10.4)]
letter = rounded_prism(A_pts, A_ROUND, A_ROUND_IN, relief_h, z_floor)
counter = rounded_prism(A_counter, 0.15, 0.0, relief_h + 0.5, z_floor - 0.1)
letter = letter.cut(counter)

plate = plate.union(rings).union(ovals).union(dots).union(letter)

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
